import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 60.0          # overall width  (X)
H = 60.0          # overall height (Z)
D = 18.3          # overall depth  (Y), open front at -Y, closed back at +Y
WALL = 3.65       # side wall thickness
FLOOR = 3.55      # back (floor) thickness
R_EDGE = 3.0      # fillet on corner edges and back perimeter

# notch through the right (+X) wall, open to the front face
NOTCH_DEPTH = 5.1     # along Y from the front face
NOTCH_HALF_Z = 14.6   # half height of the notch

# hole / boss pattern (X, Z) measured from the part centre
HOLE_X = (-15.4, 2.2)
HOLE_Z = (-15.4, 15.4)
HOLE_D = 4.5

BOSS_R_BASE = 6.08    # cone radius at the back face (before blending)
BOSS_R_TOP = 5.07     # cone radius at the top (before blending)
BOSS_H = 1.7
BOSS_FOOT_FILLET = 1.0
BOSS_TOP_FILLET = 1.0

HEX_AF = 7.7          # nut trap across flats
HEX_DEPTH = 3.25      # from the boss top

VIEW = {"azimuth": 45, "elevation": 26}

y_front = -D / 2.0
y_back = D / 2.0

# ---------------- outer shell ----------------
body = cq.Workplane("XY").box(W, D, H)
# round the 4 corner edges (parallel to Y) and the back perimeter; front stays sharp
body = body.edges("not(<Y)").fillet(R_EDGE)

# ---------------- cavity ----------------
cav_depth = D - FLOOR
cavity = (
    cq.Workplane("XY")
    .box(W - 2 * WALL, cav_depth + 1.0, H - 2 * WALL)
    .translate((0, y_front + (cav_depth - 1.0) / 2.0, 0))
)
body = body.cut(cavity)

# ---------------- notch in right wall ----------------
notch = (
    cq.Workplane("XY")
    .box(WALL + 2.0, NOTCH_DEPTH + 1.0, 2 * NOTCH_HALF_Z)
    .translate((W / 2.0 - WALL / 2.0 + 0.5, y_front + (NOTCH_DEPTH - 1.0) / 2.0, 0))
)
body = body.cut(notch)

# ---------------- bosses on the back ----------------
# low conical bosses blended into the back face (concave fillet at the foot,
# convex fillet round the top)
pts = [(x, z) for x in HOLE_X for z in HOLE_Z]
y_top = y_back + BOSS_H
for (x, z) in pts:
    cone = cq.Solid.makeCone(
        BOSS_R_BASE, BOSS_R_TOP, BOSS_H,
        pnt=cq.Vector(x, y_back, z), dir=cq.Vector(0, 1, 0),
    )
    body = body.union(cq.Workplane("XY").add(cone))


def _boss_edges(shape, y_level, radius):
    sel = []
    for e in shape.Edges():
        if e.geomType() != "CIRCLE":
            continue
        c = e.Center()
        if abs(c.y - y_level) > 1e-3:
            continue
        if abs(e.radius() - radius) > 1e-3:
            continue
        if any(abs(c.x - px) < 1e-3 and abs(c.z - pz) < 1e-3 for (px, pz) in pts):
            sel.append(e)
    return sel


solid = body.findSolid()
solid = solid.fillet(BOSS_FOOT_FILLET, _boss_edges(solid, y_back, BOSS_R_BASE))
solid = solid.fillet(BOSS_TOP_FILLET, _boss_edges(solid, y_top, BOSS_R_TOP))
body = cq.Workplane("XY").add(solid)

# ---------------- hex nut traps ----------------
R_hex = HEX_AF / math.sqrt(3.0)   # circumradius
for (x, z) in pts:
    hv = [
        (x + R_hex * math.cos(math.radians(90 + 60 * k)),
         z + R_hex * math.sin(math.radians(90 + 60 * k)))
        for k in range(6)
    ]
    hexp = (
        cq.Workplane("XZ", origin=(0, y_top + 0.5, 0))
        .polyline(hv).close()
        .extrude(HEX_DEPTH + 0.5)  # toward -Y
    )
    body = body.cut(hexp)

# ---------------- through holes ----------------
for (x, z) in pts:
    hole = (
        cq.Workplane("XZ", origin=(x, y_top + 1.0, z))
        .circle(HOLE_D / 2.0)
        .extrude(BOSS_H + FLOOR + 3.0)
    )
    body = body.cut(hole)

result = body
